import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 20.0            # outer radius of the round (eye) end
T = 34.2            # thickness (extrusion height, Z)
TIP_DX = 112.5      # distance from eye centre to wedge tip (along -X)
HOLE_R = 14.25      # through-hole radius in the eye
HOLE_FILLET = 5.0   # fillet on the top/bottom rim of the eye hole
WIN_FILLET = 4.0    # fillet on the top/bottom rim of the triangular window

# serrations on the straight (+Y) edge
N_TEETH = 18
TOOTH_PITCH = 5.73
TOOTH_FIRST_X = -104.4
TOOTH_W = 3.75      # groove width along X
TOOTH_D = 0.9       # groove depth into the edge
LAND_FILLET = 0.8   # rounding of the short lands between grooves (top & bottom)

# triangular lightening window
WALL_TOP = 6.8      # wall between window and the serrated (+Y) edge
WALL_BOT = 5.8      # wall between window and the sloped edge
RIGHT_X0 = -24.9    # x of window's end edge at y = RIGHT_Y0
RIGHT_Y0 = 5.0
RIGHT_TILT = 8.0    # tilt of the window's end edge from vertical (deg)
R_LEFT = 3.25       # corner radii of the window
R_TOPRIGHT = 2.4
R_BOTRIGHT = 2.8

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def v_add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def v_sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def v_mul(a, s):
    return (a[0] * s, a[1] * s)


def v_norm(a):
    L = math.hypot(a[0], a[1])
    return (a[0] / L, a[1] / L)


def line_intersect(p1, d1, p2, d2):
    # p1 + t d1 = p2 + s d2
    det = d1[0] * (-d2[1]) - d1[1] * (-d2[0])
    rx, ry = p2[0] - p1[0], p2[1] - p1[1]
    t = (rx * (-d2[1]) - ry * (-d2[0])) / det
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


def rounded_polygon(wp, pts, radii):
    """Closed polygon (CCW or CW) with filleted corners built from lines+arcs."""
    n = len(pts)
    corners = []
    for i in range(n):
        p = pts[i]
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        ua = v_norm(v_sub(a, p))
        ub = v_norm(v_sub(b, p))
        cosang = ua[0] * ub[0] + ua[1] * ub[1]
        ang = math.acos(max(-1.0, min(1.0, cosang)))
        r = radii[i]
        t = r / math.tan(ang / 2.0)
        pa = v_add(p, v_mul(ua, t))
        pb = v_add(p, v_mul(ub, t))
        bis = v_norm(v_add(ua, ub))
        dc = r / math.sin(ang / 2.0)
        c = v_add(p, v_mul(bis, dc))
        mid = v_add(c, v_mul(v_norm(v_sub(p, c)), r))
        corners.append((pa, mid, pb))
    w = wp.moveTo(*corners[0][2])
    for i in range(1, n + 1):
        pa, mid, pb = corners[i % n]
        w = w.lineTo(*pa).threePointArc(mid, pb)
    return w.close()


# ---------------- outer teardrop / wedge profile ----------------
# Straight serrated edge along y = +R (tangent to the eye), sloped edge tangent
# to the eye on the -Y side, meeting at a sharp tip on the -X end.
tip = (-TIP_DX, R)
d = math.hypot(TIP_DX, R)
ang_op = math.atan2(R, -TIP_DX)
alpha = math.acos(R / d)
ang_t = ang_op + alpha                      # lower tangent point angle
t2 = (R * math.cos(ang_t), R * math.sin(ang_t))

# the last groove runs out into the eye: its floor meets the circle here
y_floor = R - TOOTH_D
x_meet = -math.sqrt(R * R - y_floor * y_floor)
a1 = math.atan2(y_floor, x_meet)            # start angle of the eye arc
a2 = ang_t - 2.0 * math.pi                  # end angle (clockwise sweep)
am = 0.5 * (a1 + a2)
arc_mid = (R * math.cos(am), R * math.sin(am))

prof = cq.Workplane("XY").moveTo(*tip)
for i in range(N_TEETH):
    xc = TOOTH_FIRST_X + i * TOOTH_PITCH
    xl, xr = xc - 0.5 * TOOTH_W, xc + 0.5 * TOOTH_W
    prof = prof.lineTo(xl, R).lineTo(xl, y_floor)
    if i < N_TEETH - 1:
        prof = prof.lineTo(xr, y_floor).lineTo(xr, R)
    else:
        prof = prof.lineTo(x_meet, y_floor)
body = prof.threePointArc(arc_mid, t2).close().extrude(T)

# ---------------- eye hole ----------------
hole = cq.Workplane("XY").circle(HOLE_R).extrude(T)
body = body.cut(hole)

# ---------------- triangular window ----------------
lower_dir = v_norm(v_sub(t2, tip))                 # along the sloped edge
lower_in = (-lower_dir[1], lower_dir[0])           # inward normal (+Y side)
if lower_in[1] < 0:
    lower_in = (-lower_in[0], -lower_in[1])
top_p = (0.0, R - WALL_TOP)
top_d = (1.0, 0.0)
bot_p = v_add(tip, v_mul(lower_in, WALL_BOT))
bot_d = lower_dir
# end edge, nearly perpendicular to the wedge axis
right_d = (math.sin(math.radians(RIGHT_TILT)), math.cos(math.radians(RIGHT_TILT)))
right_p = (RIGHT_X0, RIGHT_Y0)

p_left = line_intersect(top_p, top_d, bot_p, bot_d)
p_tr = line_intersect(top_p, top_d, right_p, right_d)
p_br = line_intersect(bot_p, bot_d, right_p, right_d)

window = rounded_polygon(
    cq.Workplane("XY"), [p_left, p_tr, p_br], [R_LEFT, R_TOPRIGHT, R_BOTRIGHT]
).extrude(T)
body = body.cut(window)

# ---------------- serrations: round the short lands ----------------
# the grooves are part of the profile above; here the top/bottom edges of the
# short lands between neighbouring grooves get a small round (the long land at
# the tip stays sharp)
x_lo = TOOTH_FIRST_X
x_hi = TOOTH_FIRST_X + (N_TEETH - 1) * TOOTH_PITCH
land_edges = []
for e in body.val().Edges():
    if e.geomType() != "LINE":
        continue
    c = e.Center()
    p0, p1 = e.startPoint(), e.endPoint()
    if abs(p0.y - R) > 1e-4 or abs(p1.y - R) > 1e-4:
        continue
    if abs(p0.z - p1.z) > 1e-6 or not (abs(c.z) < 1e-4 or abs(c.z - T) < 1e-4):
        continue
    if x_lo < c.x < x_hi:
        land_edges.append(e)
body = cq.Workplane("XY").add(body.val().fillet(LAND_FILLET, land_edges))

# ---------------- fillet the cut-out rims (top and bottom) ----------------
def rim_edges(shape):
    """Edges of the inner wires (cut-out outlines) on the flat top/bottom faces."""
    hole_e, win_e = [], []
    for f in shape.Faces():
        if f.geomType() != "PLANE":
            continue
        n = f.normalAt()
        if abs(abs(n.z) - 1.0) > 1e-6:
            continue
        for w in f.innerWires():
            for e in w.Edges():
                c = e.Center()
                if math.hypot(c.x, c.y) < HOLE_R + 0.5:
                    hole_e.append(e)
                else:
                    win_e.append(e)
    return hole_e, win_e


solid = body.val()
hole_e, win_e = rim_edges(solid)
solid = solid.fillet(HOLE_FILLET, hole_e)
hole_e, win_e = rim_edges(solid)
solid = solid.fillet(WIN_FILLET, win_e)

result = cq.Workplane("XY").add(solid)
